import cadquery as cq
import math

# ======================= driving dimensions (mm) =======================
PITCH = 2.54
BOARD_W = 7 * PITCH          # 17.78
BOARD_L = 33.8
BOARD_T = 1.6
CORNER_R = 1.2
HOLE_D = 0.9
HOLE_TOP_MARGIN = 1.43       # +Y edge -> first hole row
N_SIDE = 13                  # holes along each long edge
N_END = 7                    # holes along the -Y end

# USB-C mid-mount receptacle (mouth faces +Y)
USB_W = 8.94
USB_ZBOT = -0.05
USB_ZTOP = 3.1
USB_R_TOP = 1.1
USB_R_BOT = 0.6
USB_FRONT = 17.66
USB_LEN = 6.5
USB_WALL = 0.25
USB_CAV_DEPTH = 5.2
CUT_W = 9.04                 # board cut-out width
TAB_X = 5.6                  # x of the shell legs / slots
FRONT_TAB_Y = 15.65
REAR_TAB_Y = 11.7
SLOT_W = 0.55

# QFN
QFN_S = 7.0
QFN_H = 0.9
QFN_Y = -4.4
QFN_PADS = 14
QFN_PAD_PITCH = 0.4
VIA_PITCH = 1.25

VIEW = {"azimuth": 45, "elevation": 26}

T = BOARD_T
HALF_W = BOARD_W / 2
HALF_L = BOARD_L / 2


def box(x, y, z0, w, l, h):
    """axis aligned box centred in x/y with its bottom at z0"""
    return cq.Workplane("XY").box(w, l, h, centered=(True, True, False)).translate((x, y, z0))


def solid(wp):
    return wp.val()


# ============================== board ==============================
board = (
    cq.Workplane("XY")
    .box(BOARD_W, BOARD_L, BOARD_T, centered=(True, True, False))
    .edges("|Z").fillet(CORNER_R)
)

col_x = HALF_W - PITCH / 2
top_y = HALF_L - HOLE_TOP_MARGIN
hole_pts = []
for i in range(N_SIDE):
    y = top_y - i * PITCH
    hole_pts += [(-col_x, y), (col_x, y)]
bot_y = top_y - (N_SIDE - 1) * PITCH
for i in range(1, N_END - 1):
    hole_pts.append((-col_x + i * PITCH, bot_y))
board = board.faces(">Z").workplane().pushPoints(hole_pts).hole(HOLE_D)

# 3x3 thermal vias under the QFN
via_pts = [(dx * VIA_PITCH, QFN_Y + dy * VIA_PITCH) for dx in (-1, 0, 1) for dy in (-1, 0, 1)]
board = board.faces(">Z").workplane().pushPoints(via_pts).hole(0.3)

# receptacle cut-out, open to the +Y edge
usb_rear = USB_FRONT - USB_LEN
cut_y0 = usb_rear - 0.06
board = board.cut(box(0, (cut_y0 + HALF_L + 1) / 2, -1, CUT_W, HALF_L + 1 - cut_y0, T + 2))

# slots for the shell legs
SLOTS = [(FRONT_TAB_Y, 1.8), (REAR_TAB_Y, 1.3)]
for sx in (-1, 1):
    for sy, sl in SLOTS:
        board = board.cut(
            cq.Workplane("XY").slot2D(sl, SLOT_W, angle=90).extrude(T + 2).translate((sx * TAB_X, sy, -1))
        )

board_shape = solid(board)
tools = []

# ============================ USB-C receptacle ============================
def rr_profile(y_face, w, h, rt, rb, zc):
    """rounded rectangle in the XZ plane (top radius rt, bottom radius rb)"""
    x0, x1 = -w / 2, w / 2
    z0, z1 = zc - h / 2, zc + h / 2
    c = math.cos(math.radians(45))
    return (
        cq.Workplane("XZ", origin=(0, y_face, 0))
        .moveTo(x0 + rb, z0)
        .lineTo(x1 - rb, z0)
        .threePointArc((x1 - rb + rb * c, z0 + rb - rb * c), (x1, z0 + rb))
        .lineTo(x1, z1 - rt)
        .threePointArc((x1 - rt + rt * c, z1 - rt + rt * c), (x1 - rt, z1))
        .lineTo(x0 + rt, z1)
        .threePointArc((x0 + rt - rt * c, z1 - rt + rt * c), (x0, z1 - rt))
        .lineTo(x0, z0 + rb)
        .threePointArc((x0 + rb - rb * c, z0 + rb - rb * c), (x0 + rb, z0))
        .close()
    )


usb_h = USB_ZTOP - USB_ZBOT
usb_zc = (USB_ZBOT + USB_ZTOP) / 2
shell = rr_profile(USB_FRONT, USB_W, usb_h, USB_R_TOP, USB_R_BOT, usb_zc).extrude(USB_LEN)

# mouth cavity with a lead-in funnel
cav_w = USB_W - 2 * USB_WALL
cav_h = usb_h - 2 * USB_WALL
cav_rt = USB_R_TOP - USB_WALL
cav_rb = USB_R_BOT - USB_WALL
cavity = rr_profile(USB_FRONT + 0.01, cav_w, cav_h, cav_rt, cav_rb, usb_zc).extrude(USB_CAV_DEPTH)
FUNNEL = 0.12
funnel = rr_profile(USB_FRONT + 0.001, cav_w + 2 * FUNNEL, cav_h + 2 * FUNNEL,
                    cav_rt + FUNNEL, cav_rb + FUNNEL, usb_zc).extrude(FUNNEL, taper=45)
shell = shell.cut(cavity).cut(funnel)

# recessed moulded housing at the rear (shell sheet edge stands proud)
REAR_RECESS = 0.25
rear_recess = rr_profile(usb_rear - 0.01, cav_w, cav_h, cav_rt, cav_rb, usb_zc).extrude(-(REAR_RECESS + 0.01))
shell = shell.cut(rear_recess)

# tongue
tongue_len = USB_CAV_DEPTH - 0.7
tongue = box(0, USB_FRONT - 0.7 - tongue_len / 2, usb_zc - 0.35, 6.6, tongue_len, 0.7)
shell = shell.union(tongue)

# windows in the rear of the top sheet with bent-down latches
NOTCH_D = 0.6
for nx in (-1.85, 1.71):
    shell = shell.cut(box(nx, usb_rear + 0.6, USB_ZTOP - NOTCH_D, 1.9, 1.25, 1.0))
    yf, yr = usb_rear + 1.26, usb_rear + 0.05
    zf = USB_ZTOP - NOTCH_D - 0.02
    latch = (
        cq.Workplane("YZ", origin=(nx - 0.6, 0, 0))
        .polyline([(yf, USB_ZTOP - 0.02), (yf, USB_ZTOP - 0.2),
                   (yr + 0.2, zf), (yr, zf), (yr, zf + 0.12)])
        .close()
        .extrude(1.2)
    )
    shell = shell.union(latch)
# stamped dimple on top
dimple = cq.Solid.makeCone(0.0, 0.8, 0.2, pnt=cq.Vector(0, usb_rear + 1.7, USB_ZTOP - 0.15),
                           dir=cq.Vector(0, 0, 1))
shell = shell.cut(cq.Workplane("XY").add(dimple))
# stamping slits (round-topped) in the side walls next to the legs
SLITS = [FRONT_TAB_Y - 0.75, FRONT_TAB_Y + 0.75, REAR_TAB_Y + 0.7]
for sx in (-1, 1):
    for sy in SLITS:
        slit = (
            cq.Workplane("YZ", origin=(sx * USB_W / 2 - 0.4, 0, 0))
            .center(sy, T + 0.3)
            .slot2D(0.75, 0.14, angle=90)
            .extrude(0.8)
        )
        shell = shell.cut(slit)

# dovetail seam of the rolled shell along the bottom centre
seam = []
seam_pts = [(-0.25, usb_rear + 0.9), (-0.25, usb_rear + 2.3), (0.25, usb_rear + 2.3),
            (0.25, usb_rear + 3.6), (-0.25, usb_rear + 3.6), (-0.25, USB_FRONT + 0.1)]
for (xa, ya), (xb, yb) in zip(seam_pts[:-1], seam_pts[1:]):
    w = abs(xb - xa) + 0.06
    l = abs(yb - ya) + 0.06
    seam.append(solid(box((xa + xb) / 2, (ya + yb) / 2, USB_ZBOT - 0.01, w, l, 0.05)))
# spring-latch windows stamped in the bottom sheet near the mouth
for sx in (-1, 1):
    seam.append(solid(box(sx * 2.7, USB_FRONT - 1.2, USB_ZBOT - 0.01, 1.4, 1.3, 0.11)))
shell = cq.Workplane("XY").add(solid(shell).cut(*seam))

usb_parts = [solid(shell)]


def bent_leg(side, yc, width):
    """sheet-metal leg: leaves the shell wall, runs outward and bends down into the slot"""
    x_in = side * (USB_W / 2 - 0.12)
    x_b = side * (TAB_X - 0.22)
    z_h = T + 0.32
    path = (
        cq.Workplane("XZ", origin=(0, yc + width / 2, 0))
        .moveTo(x_in, z_h)
        .lineTo(x_b, z_h)
        .threePointArc((x_b + side * 0.156, z_h - 0.064), (side * TAB_X, z_h - 0.22))
        .lineTo(side * TAB_X, 0.15)
    )
    return solid(path.offset2D(0.075, kind="intersection").extrude(width))


for sx in (-1, 1):
    # front leg: forked, two strips
    for dy in (-0.38, 0.38):
        usb_parts.append(bent_leg(sx, FRONT_TAB_Y + dy, 0.3))
    # rear leg: single wide strip
    usb_parts.append(bent_leg(sx, REAR_TAB_Y, 0.9))

# SMT signal pins at the rear
N_PINS = 14
for i in range(N_PINS):
    px = (i - (N_PINS - 1) / 2) * 0.5
    usb_parts.append(solid(box(px, usb_rear - 0.15, T, 0.25, 1.0, 0.1)))

usb = usb_parts[0].fuse(*usb_parts[1:])
tools.append(usb)


# ============================== components ==============================
def chip_part(x, y, vertical=False, L=1.0, W=0.5, H=0.36, cap=0.22, fr=0.03):
    """chip resistor / capacitor: two metallised end caps and a slightly smaller body"""
    pieces = []
    for s in (-1, 1):
        c = L / 2 - cap / 2
        if vertical:
            b = box(x, y + s * c, T, W, cap, H)
        else:
            b = box(x + s * c, y, T, cap, W, H)
        pieces.append(solid(b.edges("not <Z").fillet(fr)))
    bl = L - 2 * cap + 0.02
    if vertical:
        body = box(x, y, T, W - 0.04, bl, H - 0.04)
    else:
        body = box(x, y, T, bl, W - 0.04, H - 0.04)
    return pieces[0].fuse(pieces[1], solid(body))


PASSIVES_H = [
    (-2.48, 7.99), (1.90, 7.99), (5.26, 5.89), (-3.15, 4.99), (-0.99, 4.99),
    (-0.99, 4.03), (-0.99, 3.08), (-5.14, -9.15), (5.04, -9.15),
    (2.18, -9.9), (2.18, -10.82), (2.18, -11.73),
    (-1.89, -13.35), (0.13, -13.35),
]
PASSIVES_V = [
    (1.62, 3.59), (-4.63, -1.35), (4.54, -1.27), (5.46, -1.27), (4.62, -4.91),
    (-4.69, -6.0), (0.78, -11.53),
]
ROW_X0, ROW_X1, ROW_Y = -0.57, 5.04, 0.98
for i in range(7):
    PASSIVES_V.append((ROW_X0 + i * (ROW_X1 - ROW_X0) / 6, ROW_Y))

for (x, y) in PASSIVES_H:
    tools.append(chip_part(x, y, False))
for (x, y) in PASSIVES_V:
    tools.append(chip_part(x, y, True))

# 0805 chip part
tools.append(chip_part(-2.39, 6.59, False, L=2.0, W=1.25, H=0.45, cap=0.35, fr=0.04))

# small LED / SOD-523 style part: moulded body on a wider terminal base
LX, LY = 2.18, -12.65
led = box(LX, LY, T, 1.0, 0.5, 0.12)
led_body = box(LX - 0.05, LY, T + 0.1, 0.75, 0.5, 0.33).edges(">Z").fillet(0.08)
tools.append(solid(led).fuse(solid(led_body)))

# SOD-323 diode, leads along X
dx_, dy_ = 1.11, 6.59
sod = box(dx_, dy_, T + 0.05, 1.7, 1.25, 0.72)
for s in (-1, 1):
    sod = sod.union(box(dx_ + s * 1.05, dy_, T, 0.5, 0.3, 0.12))
tools.append(solid(sod))


# SOT-23-5: two-tier moulded body with draft, gull-wing leads
def tapered_block(x, y, z0, w, l, h, taper_deg):
    return (
        cq.Workplane("XY", origin=(x, y, z0))
        .rect(w, l)
        .extrude(h, taper=taper_deg)
    )


SOT_X, SOT_Y = 4.16, 3.70
SOT_W, SOT_L = 1.6, 2.9
SOT_PART = T + 0.8
lower = tapered_block(SOT_X, SOT_Y, SOT_PART, SOT_W, SOT_L, 0.72, 8).mirror(
    "XY", basePointVector=(0, 0, SOT_PART))
upper = tapered_block(SOT_X, SOT_Y, SOT_PART, SOT_W, SOT_L, 0.65, 8)
sot_parts = [solid(lower), solid(upper)]


def gull_lead(x_root, y, side):
    """gull-wing lead profile in XZ, extruded 0.4 mm along Y"""
    z_top = SOT_PART - 0.05
    x0 = x_root - side * 0.1
    path = (
        cq.Workplane("XZ", origin=(0, y + 0.2, 0))
        .moveTo(x0, z_top)
        .lineTo(x_root + side * 0.15, z_top)
        .threePointArc((x_root + side * 0.28, z_top - 0.06), (x_root + side * 0.33, z_top - 0.2))
        .lineTo(x_root + side * 0.33, T + 0.2)
        .threePointArc((x_root + side * 0.38, T + 0.11), (x_root + side * 0.52, T + 0.06))
        .lineTo(x_root + side * 0.78, T + 0.06)
    )
    prof = path.offset2D(0.07, kind="intersection")
    return solid(prof.extrude(0.4))


for side, ys in ((1, (-0.95, 0.0, 0.95)), (-1, (-0.95, 0.95))):
    for dyl in ys:
        sot_parts.append(gull_lead(SOT_X + side * SOT_W / 2, SOT_Y + dyl, side))
tools.append(sot_parts[0].fuse(*sot_parts[1:]))

# 3 x 4 mm DFN / module with castellated edges and pin-1 dimple
CX, CY = -3.65, 1.95
CW, CL, CH = 3.05, 3.95, 1.0
chip = box(CX, CY, T, CW, CL, CH)
cast = []
for i in range(5):
    py = CY - 1.3 + i * 0.65
    for s in (-1, 1):
        cast.append(solid(box(CX + s * CW / 2, py, T - 0.01, 0.3, 0.22, 0.2)))
cast.append(cq.Solid.makeSphere(0.18, angleDegrees1=-90).translate(cq.Vector(CX - 1.15, CY + 1.6, T + CH + 0.08)))
tools.append(solid(chip).cut(*cast))

# 7 x 7 QFN with side pads
qfn = box(0, QFN_Y, T, QFN_S, QFN_S, QFN_H)
pad_cuts = []
for i in range(QFN_PADS):
    d = (i - (QFN_PADS - 1) / 2) * QFN_PAD_PITCH
    pad_cuts += [
        solid(box(d, QFN_Y - QFN_S / 2, T - 0.01, 0.12, 0.1, 0.18)),
        solid(box(d, QFN_Y + QFN_S / 2, T - 0.01, 0.12, 0.1, 0.18)),
        solid(box(-QFN_S / 2, QFN_Y + d, T - 0.01, 0.1, 0.12, 0.18)),
        solid(box(QFN_S / 2, QFN_Y + d, T - 0.01, 0.1, 0.12, 0.18)),
    ]
qfn_shape = solid(qfn).cut(*pad_cuts)
tools.append(qfn_shape)

# ============================== assemble ==============================
fused = board_shape.fuse(*tools).clean()
result = cq.Workplane("XY").add(fused)
